import cadquery as cq

# ------------------------------------------------------------------
# Hemispherical bowl (one half of a spherical shell) whose flat rim
# carries an annular groove (lip/groove joint for a mating half).
# The rim face lies (practically) at Z = 0, the bowl hangs below it.
# ------------------------------------------------------------------
R_out = 50.0          # outer sphere radius
wall = 2.9            # shell wall thickness
w_land_out = 0.65     # width of the outer land on the rim face
w_groove = 1.45       # radial width of the rim groove
d_groove = 2.5        # depth of the rim groove
rim_drop = 0.05       # rim face sits this far below the equator so the
                      # sphere poles (on the equator) stay off the part

R_in = R_out - wall               # inner sphere radius
R_g_out = R_out - w_land_out      # groove outer wall radius
R_g_in = R_g_out - w_groove       # groove inner wall radius

big = 4 * R_out


def sphere(r):
    # Sphere whose axis lies along X: its seam meridian runs through the
    # upper (removed) half and its poles sit on the equator, so the kept
    # lower part is a single clean spherical patch.
    return cq.Workplane("XY").add(
        cq.Solid.makeSphere(r, cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -90, 90, 360)
    )


def below(z):
    # half-space below the plane Z = z
    return cq.Workplane("XY").box(big, big, big, centered=(True, True, False)).translate(
        (0, 0, z - big)
    )


# hemispherical shell, open at the top, rim face at Z = -rim_drop
shell = sphere(R_out).intersect(below(-rim_drop)).cut(sphere(R_in))

# annular groove cut down into the rim face (walls concentric with the bowl)
groove_ring = sphere(R_g_out).cut(sphere(R_g_in))
groove = groove_ring.cut(below(-rim_drop - d_groove))

result = shell.cut(groove)

VIEW = {"azimuth": 45, "elevation": 26}
